import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
N_SIDES = 9              # nonagonal bipyramid -> 18 faces (d18 die)
R = 20.0                 # circumradius of the equatorial nonagon
H = 0.965 * R            # apex height above / below the equator
DIGIT_H = 0.225 * R      # cap height of the engraved digits
TEXT_DEPTH = 0.022 * R   # engraving depth
TEXT_POS = 0.665         # number centre: fraction of the way apex -> edge midpoint
FIRST_VERTEX_DEG = 90.0  # one equator vertex points to +Y

# Arial-like spacing, expressed in "em" of a font whose cap height is 0.716 em
EM = DIGIT_H / 0.716
DIGIT_ADV = 0.556 * EM
DOT_ADV = 0.278 * EM
KERN_11 = -0.074 * EM    # Arial kerns the pair "11"

# face numbers, counter-clockwise (seen from above) starting at the -Y face
TOP_NUMBERS = ["7", "9.", "11", "13", "15", "17", "1", "3", "5"]
BOT_NUMBERS = ["12", "10", "8", "6.", "4", "2", "18", "16", "14"]


def V(x, y, z):
    return cq.Vector(x, y, z)


# ---------------- the bipyramid ----------------
eq = []
for k in range(N_SIDES):
    a = math.radians(FIRST_VERTEX_DEG + k * 360.0 / N_SIDES)
    eq.append(V(R * math.cos(a), R * math.sin(a), 0.0))

top = V(0, 0, H)
bot = V(0, 0, -H)


def tri(p0, p1, p2):
    w = cq.Wire.makePolygon([p0, p1, p2], close=True)
    return cq.Face.makeFromWires(w)


faces = []
for k in range(N_SIDES):
    p0, p1 = eq[k], eq[(k + 1) % N_SIDES]
    faces.append(tri(p0, p1, top))
    faces.append(tri(p1, p0, bot))
die = cq.Solid.makeSolid(cq.Shell.makeShell(faces))
if die.Volume() < 0:
    die = cq.Solid(die.wrapped.Reversed())


# ---------------- engraved numbers ----------------
def glyph_one(x0, ext):
    """Sans-serif '1' without a foot (Arial style), baseline at y = 0."""
    def p(x, y):
        return (x0 + x * EM, y * EM)

    s = (cq.Workplane("XY")
         .moveTo(*p(0.3726, 0.0))
         .lineTo(*p(0.3726, 0.7158))
         .lineTo(*p(0.3145, 0.7158))
         .threePointArc(p(0.232, 0.618), p(0.1089, 0.5391))
         .lineTo(*p(0.1089, 0.4541))
         .threePointArc(p(0.205, 0.498), p(0.2847, 0.5601))
         .lineTo(*p(0.2847, 0.0))
         .close()
         .extrude(ext))
    return s.val()


def glyph_seven(x0, ext):
    """Sans-serif '7' with a curved stem (Arial style), baseline at y = 0."""
    def p(x, y):
        return (x0 + x * EM, y * EM)

    s = (cq.Workplane("XY")
         .moveTo(*p(0.047, 0.631))
         .lineTo(*p(0.047, 0.7158))
         .lineTo(*p(0.511, 0.7158))
         .lineTo(*p(0.511, 0.647))
         .threePointArc(p(0.300, 0.330), p(0.236, 0.0))
         .lineTo(*p(0.148, 0.0))
         .threePointArc(p(0.212, 0.340), p(0.421, 0.631))
         .close()
         .extrude(ext))
    return s.val()


FONT = "DejaVu Sans"
DV_SIZE = DIGIT_H / 0.729   # DejaVu Sans digit height is 0.729 em


def glyph(ch, x0, ext):
    if ch == "1":
        return glyph_one(x0, ext)
    if ch == "7":
        return glyph_seven(x0, ext)
    s = cq.Workplane("XY").text(ch, DV_SIZE, ext, font=FONT,
                                halign="left", valign="bottom").val()
    bb = s.BoundingBox()
    adv = DOT_ADV if ch == "." else DIGIT_ADV
    if ch == ".":
        cx = x0 + 0.1365 * EM
    else:
        cx = x0 + adv / 2.0
    return s.translate(V(cx - (bb.xmin + bb.xmax) / 2.0, 0, 0))


def advances(txt):
    """x position of every character and the total advance of the string."""
    xs = []
    x = 0.0
    prev = ""
    for ch in txt:
        if prev == "1" and ch == "1":
            x += KERN_11
        xs.append(x)
        x += DOT_ADV if ch == "." else DIGIT_ADV
        prev = ch
    return xs, x


def number_solids(txt, ext):
    xs, _ = advances(txt)
    out = []
    for ch, x in zip(txt, xs):
        try:
            out.append(glyph(ch, x, ext))
        except Exception:
            pass  # no usable system font: leave that glyph out
    return out


def number_cutter(txt, apex, a, b):
    """Engraving tool for face (a, b, apex); text 'up' points to the apex."""
    m = (a + b) * 0.5
    n = (a - apex).cross(b - apex).normalized()
    if n.dot(m) < 0:
        n = -n
    u = (apex - m).normalized()
    r = u.cross(n).normalized()
    c = apex + (m - apex) * TEXT_POS
    parts = number_solids(txt, TEXT_DEPTH * 2.0)
    comp = cq.Compound.makeCompound(parts)
    _, width = advances(txt)
    # centred on the advance box of the string, like a CAD text tool does
    comp = comp.translate(V(-width / 2.0, -DIGIT_H / 2.0, -TEXT_DEPTH))
    pl = cq.Plane(origin=c, xDir=r, normal=n)
    return [s.moved(cq.Location(pl)) for s in comp.Solids()]


cutters = []
for k in range(N_SIDES):
    # face between equator vertices idx and idx+1 has its centre direction at
    # FIRST_VERTEX_DEG + (idx + 0.5) * 40 deg; idx = 4 is the -Y face.
    idx = (k + 4) % N_SIDES
    p0, p1 = eq[idx], eq[(idx + 1) % N_SIDES]
    cutters += number_cutter(TOP_NUMBERS[k], top, p0, p1)
    cutters += number_cutter(BOT_NUMBERS[k], bot, p0, p1)

tool = cq.Compound.makeCompound(cutters)
engraved = die.cut(tool)
solids = engraved.Solids()
solid = max(solids, key=lambda x: x.Volume())
result = cq.Workplane("XY").add(solid)

VIEW = {"azimuth": 45, "elevation": 26}
